import math
import cadquery as cq

# Bust of a boy in a hoodie, head bowed.  Built in a local frame
# (x = bust's right, y = facing direction, z = up, base on z = 0) and then
# turned TURN degrees about Z so it faces the back-left camera.

# ---------------- driving dimensions (mm) ----------------
TURN = 45.0

# torso: back/hood mass + two shoulder masses (half ellipsoids on the base plane)
# (centres sit 2 mm under the base so the ellipsoid poles/seams are cut away)
BACK_C, BACK_AX = (-2.0, -24.0, -2.0), (66.0, 40.0, 44.0)
HOOD_C, HOOD_AX, HOOD_TILT = (-4.0, -34.0, 12.0), (44.0, 42.0, 26.0), -20.0   # hood lying on the back
SHL_L_C, SHL_L_AX, SHL_L_YAW = (-60.0, -6.5, -2.0), (48.0, 36.0, 35.0), 0.0
SHL_R_C, SHL_R_AX, SHL_R_YAW = (55.0, -10.0, -2.0), (36.0, 32.0, 35.0), 0.0
TRAP_X, TRAP_Y, TRAP_AX = 30.0, -5.0, (35.0, 30.0, 44.0)   # yoke either side of the neck
TORSO_BLEND = 10.0

# hood opening: a round lip swept round the back of the neck, ends running
# down into the chest as the V of the opening
COLLAR_r = 10.0
COLLAR_PATH = [(24, 17, -8), (36, 24, 18), (47, 10, 32), (45, -15, 36), (24, -27, 29), (0, -29, 27),
               (-24, -27, 29), (-46, -15, 36), (-48, 10, 32), (-37, 24, 18), (-25, 17, -8)]

# neck (lofted ellipses): (z, cx, cy, semi_x, semi_y)
NECK_SECTIONS = [
    (-5.0, 1.0, 0.0, 38.0, 30.0),
    (60.0, 2.0, 18.0, 36.0, 31.0),
    (104.0, 4.0, 27.0, 41.0, 33.0),
]
NECK_BLEND = 8.0

# head
HEAD_TILT = 20.0
CRANIUM_C, CRANIUM_AX, CRANIUM_TILT = (8.5, 24.7, 134.3), (60.0, 72.8, 64.4), 26.8
FACE_C, FACE_AX, FACE_TILT = (3.0, 48.0, 82.0), (45.0, 32.0, 44.0), 20.0
OCCIPUT_C, OCCIPUT_AX = (7.0, -5.0, 100.0), (38.0, 20.0, 24.0)
FACE_CUT_C, FACE_CUT_AX = (3.0, 110.0, 74.0), (82.0, 46.0, 48.0)   # clears the hair off the face
EYE_AX = (10.0, 5.0, 5.0)            # eye sockets
EYE_L_C, EYE_R_C = (-15.0, 77.0, 101.0), (21.0, 77.0, 101.0)
NOSE_BRIDGE_C, NOSE_BRIDGE_AX = (2.0, 83.0, 101.0), (5.5, 7.0, 14.0)
NOSE_TIP_C, NOSE_TIP_AX = (2.0, 85.0, 87.0), (9.5, 7.0, 6.5)
NOSE_TILT = 30.0
EAR_L_C = (-45.5, 11.0, 106.0)
EAR_R_C = (57.5, 9.0, 100.0)
EAR_AX = (5.0, 10.0, 18.0)
EAR_CUP_AX = (3.0, 6.0, 11.0)        # hollow of the ear
EAR_FLARE = 30.0                     # back edge of the ear turned out (deg)


def ellipsoid(center, axes, tilt_x=0.0, yaw=0.0, poles="y"):
    """Ellipsoid with semi axes `axes`, pitched forward by tilt_x deg, turned yaw deg, centred at `center`.
    poles="y": poles front/back with the seam meridian underneath (hidden or cut away);
    poles="z": poles top/bottom, seam on the +x side; "zb": seam at the back."""
    s = cq.Solid.makeSphere(1.0, angleDegrees1=-90, angleDegrees2=90, angleDegrees3=360)
    if poles == "y":
        s = s.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), -90).rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), 90)
    elif poles == "zb":
        s = s.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), -90)
    elif poles == "x":
        s = s.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), 90)
    a, b, c = axes
    s = s.transformGeometry(cq.Matrix([[a, 0, 0, 0], [0, b, 0, 0], [0, 0, c, 0]]))
    if tilt_x:
        s = s.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), -tilt_x)
    if yaw:
        s = s.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), yaw)
    return s.translate(cq.Vector(*center))


def ellipse_wire(cx, cy, z, a, b):
    if a >= b:
        return cq.Wire.makeEllipse(a, b, cq.Vector(cx, cy, z), cq.Vector(0, 0, 1), cq.Vector(1, 0, 0))
    return cq.Wire.makeEllipse(b, a, cq.Vector(cx, cy, z), cq.Vector(0, 0, 1), cq.Vector(0, 1, 0))


def tube(points, r):
    edge = cq.Workplane("XY").spline(points, includeCurrent=False).val()
    path = cq.Wire.assembleEdges([edge])
    t = edge.tangentAt(0)
    plane = cq.Plane(origin=edge.startPoint(), xDir=cq.Vector(0, 0, 1).cross(t).normalized(), normal=t)
    return cq.Workplane(plane).circle(r).sweep(cq.Workplane().add(path)).val()


def sharp_edges(s, min_angle=8.0):
    """edges where two faces meet at a crease (seams and tangent joins skipped)"""
    faces = s.Faces()
    owners = {}
    for fi, f in enumerate(faces):
        for e in f.Edges():
            owners.setdefault(e.hashCode(), []).append((fi, e))
    out = []
    for lst in owners.values():
        fis = sorted(set(fi for fi, _ in lst))
        if len(fis) != 2:
            continue
        e = lst[0][1]
        p = e.positionAt(0.5)
        ang = math.degrees(faces[fis[0]].normalAt(p).getAngle(faces[fis[1]].normalAt(p)))
        if ang > min_angle:
            out.append(e)
    return out


def blend(s, r, zmin=None):
    """fillet the creases left by a boolean union, backing off the radius if OCC refuses"""
    es = sharp_edges(s)
    if zmin is not None:
        es = [e for e in es if e.Center().z > zmin]
    if not es:
        return s
    for rr in (r, 0.7 * r, 0.5 * r, 0.35 * r):
        try:
            f = s.fillet(rr, es)
            if f.isValid():
                return f
        except Exception:
            pass
    return s


def ear(center, side):
    """ear: flattened ellipsoid with a hollow on its outer face, back edge flared out"""
    e = ellipsoid((0, 0, 0), EAR_AX, poles="z")
    cup = ellipsoid((side * (EAR_AX[0] - 0.5), 1.0, 0.0), EAR_CUP_AX, poles="z")
    e = e.cut(cup)
    e = e.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), side * EAR_FLARE)
    return e.translate(cq.Vector(*center))


def fuse(a, b):
    return a.fuse(b).clean()


# ---------------- torso ----------------
torso = fuse(ellipsoid(BACK_C, BACK_AX), ellipsoid(SHL_L_C, SHL_L_AX, yaw=SHL_L_YAW))
torso = fuse(torso, ellipsoid(SHL_R_C, SHL_R_AX, yaw=SHL_R_YAW))
for side in (-1, 1):
    torso = fuse(torso, ellipsoid((side * TRAP_X + 2.0, TRAP_Y, -2.0), TRAP_AX))
torso = fuse(torso, ellipsoid(HOOD_C, HOOD_AX, HOOD_TILT))
torso = blend(torso, TORSO_BLEND, zmin=1.0)
torso = fuse(torso, tube(COLLAR_PATH, COLLAR_r))

neck = cq.Solid.makeLoft([ellipse_wire(cx, cy, z, a, b) for (z, cx, cy, a, b) in NECK_SECTIONS], False)

# ---------------- head ----------------
head = ellipsoid(CRANIUM_C, CRANIUM_AX, CRANIUM_TILT).cut(ellipsoid(FACE_CUT_C, FACE_CUT_AX))
head = blend(head, 2.0)
face = ellipsoid(FACE_C, FACE_AX, FACE_TILT, poles="zb")
face = face.cut(ellipsoid(EYE_L_C, EYE_AX, HEAD_TILT, poles="z")).cut(ellipsoid(EYE_R_C, EYE_AX, HEAD_TILT, poles="z"))
head = fuse(head, face)
head = fuse(head, ellipsoid(OCCIPUT_C, OCCIPUT_AX))
nose = fuse(ellipsoid(NOSE_BRIDGE_C, NOSE_BRIDGE_AX, NOSE_TILT, poles="z"),
            ellipsoid(NOSE_TIP_C, NOSE_TIP_AX, NOSE_TILT, poles="z"))

# ---------------- assembly of the features ----------------
body = fuse(torso, neck)
body = fuse(body, head)
body = fuse(body, nose)
body = fuse(fuse(body, ear(EAR_L_C, -1)), ear(EAR_R_C, 1))

# flat base
big = cq.Solid.makeBox(600, 600, 600, pnt=cq.Vector(-300, -300, 0))
body = body.intersect(big).clean()
body = body.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), TURN)

result = cq.Workplane("XY").add(body)
